import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 70.0          # overall width  (X)
D = 50.0          # overall depth  (Y)
H = 59.0          # overall height (Z)
T = 2.0           # wall thickness
R_VERT = 2.5      # outer radius of the vertical corner edges
R_TOP = 3.0       # outer radius of the top edges
R_IN_VERT = 1.0   # inner radius of the vertical corner edges
R_IN_TOP = 1.0    # inner radius of the top edges
R_BOT_OUT = 1.5   # round on the outer bottom edge of the side (+/-X) walls
R_BOT_IN = 0.4    # round on the inner bottom edge of the walls

# front (-Y) wall arch cut-out (large)
ARCH_F_R = 37.3
ARCH_F_ZC = -13.6
# back (+Y) wall arch cut-out (small)
ARCH_B_R = 23.4
ARCH_B_ZC = -14.3

# peanut / figure-8 hole in the left (-X) wall: two circles with rounded waist
F8_R = 6.6        # lobe radius
F8_DY = 5.9       # half spacing of lobe centres along Y
F8_Z = 9.9        # lobe centre height
F8_RF = 1.2       # waist round radius

# rectangular window in the right (+X) wall
SQ_W = 10.1       # along Y
SQ_H = 10.8       # along Z
SQ_Y = 5.6
SQ_Z = 15.9

# ---------------- body: open-bottom rounded box ----------------
outer = (
    cq.Workplane("XY")
    .box(W, D, H, centered=(True, True, False))
    .edges(">Z").fillet(R_TOP)
    .edges("|Z").fillet(R_VERT)
)
inner = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .box(W - 2 * T, D - 2 * T, H - T + 1.0, centered=(True, True, False))
    .edges("|Z").fillet(R_IN_VERT)
    .edges(">Z").fillet(R_IN_TOP)
)
body = outer.cut(inner)

# ---------------- bottom rim treatment ----------------
# small round on the inner bottom edge all the way round
bottom_face = body.faces("<Z").val()
inner_loop = [e for w in bottom_face.innerWires() for e in w.Edges()]
solid = body.val().fillet(R_BOT_IN, inner_loop)
body = cq.Workplane("XY").newObject([solid])

# outer bottom edge of the two side walls (+/-X) rounded by a straight
# Y-direction cutter (it runs out on the corner bends, back/front stay sharp)
for sx in (-1, 1):
    xc = sx * (W / 2 - R_BOT_OUT)
    block = (
        cq.Workplane("XZ", origin=(0, D / 2 + 1.0, 0))
        .center(sx * (W / 2 - R_BOT_OUT / 2 + 0.5), (R_BOT_OUT - 1.0) / 2)
        .rect(R_BOT_OUT + 1.0, R_BOT_OUT + 1.0)
        .extrude(D + 2.0)
    )
    rod = (
        cq.Workplane("XZ", origin=(0, D / 2 + 2.0, 0))
        .center(xc, R_BOT_OUT)
        .circle(R_BOT_OUT)
        .extrude(D + 4.0)
    )
    body = body.cut(block.cut(rod))

# ---------------- front arch (through front wall only) ----------------
arch_f = (
    cq.Workplane("XZ", origin=(0, -D / 2 - 1.0, 0))
    .center(0, ARCH_F_ZC)
    .circle(ARCH_F_R)
    .extrude(-(T + 1.0))
)
body = body.cut(arch_f)

# ---------------- back arch (through back wall only) ----------------
arch_b = (
    cq.Workplane("XZ", origin=(0, D / 2 - T, 0))
    .center(0, ARCH_B_ZC)
    .circle(ARCH_B_R)
    .extrude(-(T + 1.0))
)
body = body.cut(arch_b)

# ---------------- peanut hole in left wall ----------------
s, R, rf = F8_DY, F8_R, F8_RF
yc = math.sqrt((R + rf) ** 2 - s ** 2)   # height of the waist-round centres
k = R / (R + rf)
tx = s - k * s                           # tangent point lobe / waist round (u)
tv = k * yc                              # tangent point lobe / waist round (v)
neck = yc - rf                           # half width of the waist
f8 = (
    cq.Workplane("YZ", origin=(-W / 2 - 1.0, 0, F8_Z))
    .moveTo(tx, tv)
    .threePointArc((s + R, 0.0), (tx, -tv))
    .threePointArc((0.0, -neck), (-tx, -tv))
    .threePointArc((-s - R, 0.0), (-tx, tv))
    .threePointArc((0.0, neck), (tx, tv))
    .close()
    .extrude(T + 1.5)
)
body = body.cut(f8)

# ---------------- rectangular window in right wall ----------------
sq = (
    cq.Workplane("YZ", origin=(W / 2 - T - 0.5, 0, 0))
    .center(SQ_Y, SQ_Z)
    .rect(SQ_W, SQ_H)
    .extrude(T + 1.5)
)
body = body.cut(sq)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
